import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 120.0          # overall length (X)
W = 51.7           # overall width (Y)
H = 11.9           # overall height incl. lip (Z)
CH_X = 6.5         # corner chamfer run along X
CH_Y = 12.9        # corner chamfer run along Y
R_CORNER = 1.8     # plan-view rounding of outer corners
LIP_CORNER_R = 1.2

LIP_H = 2.1        # height of the top lip
LEDGE = 1.5        # step from outer wall to lip
WALL = 3.1         # total wall thickness (outer wall -> cavity)
TOP_EDGE_R = 0.5   # rounding of outer wall top edge

FLOOR_T = 2.6      # floor thickness
FLOOR_FILLET = 2.0 # cavity floor/wall fillet
CAV_CORNER_R = 1.0 # cavity vertical corner fillet

BOT_ARC_Z = 5.2    # height where bottom rounding starts on the outer wall
BOT_ARC_IN = 2.5   # inset of the rounding at the bottom face

# bosses (stand-offs with locating pins)
BOSS_X_L = -45.35
BOSS_X_R = 45.0
BOSS_Y_POS = 16.7
BOSS_Y_NEG = -14.75
BOSS_D = 6.3
BOSS_TOP = 9.7
BOSS_TOP_R = 0.5
BOSS_BASE_R = 1.5
PIN_D = 3.6
PIN_TOP = 11.2
PIN_HOLE_D = 2.4
PIN_HOLE_BOT = 4.0

# rectangular window
WIN_CX, WIN_CY = -14.7, -0.5
WIN_W, WIN_H = 38.6, 20.8
WIN_R = 1.5
WIN_EDGE_R = 0.4
WIN_BOT_CH = 1.2

# square recess with round hole
SQ_CX, SQ_CY = 24.2, 0.0
SQ_W, SQ_H = 19.0, 21.75
SQ_R = 1.2
SQ_DEPTH = 1.4
HOLE_D = 10.3
HOLE_BOT_CH = 0.5

# hex pocket (nut trap) with channel, top floor
HEX_CX, HEX_CY = 47.1, 6.8
HEX_R = 7.8
HEX_DEPTH = 1.2
CHAN_X0, CHAN_X1 = 49.5, 53.7
CHAN_Y1 = 16.2
CHAN_DEPTH = 1.0

# vent slots
SLOT_W = 0.9
SLOTS = [((41.5, -3.65), (45.95, -8.9)),
         ((40.9, -6.35), (43.4, -8.9)),
         ((44.2, -3.45), (46.6, -6.15))]

# bottom logo recesses
LOGO_DEPTH = 0.4
LOGO1 = (47.1, 6.8, 7.6)     # x, y, circumradius  (+X end, with channel + cross)
LOGO2 = (-47.6, 1.4, 9.0)    # -X end, with letter bars
CROSS_L, CROSS_W = 8.4, 1.2
LOGO_TEXT_ANG = 38.0
STROKE = 0.9

Z_WALL = H - LIP_H  # top of outer wall / ledge level


# ---------------- helpers ----------------
def poly_lines(d):
    """outward normals + offsets of the 8 outline edges, offset inward by d"""
    a, b = L / 2.0, W / 2.0
    nrm = math.hypot(CH_X, CH_Y)
    lines = []
    lines.append(((0.0, -1.0), b))                                   # bottom
    n = (CH_Y / nrm, -CH_X / nrm)
    lines.append((n, n[0] * a + n[1] * (-b + CH_Y)))                 # BR chamfer
    lines.append(((1.0, 0.0), a))                                    # right
    n = (CH_Y / nrm, CH_X / nrm)
    lines.append((n, n[0] * a + n[1] * (b - CH_Y)))                  # TR chamfer
    lines.append(((0.0, 1.0), b))                                    # top
    n = (-CH_Y / nrm, CH_X / nrm)
    lines.append((n, n[0] * (-a) + n[1] * (b - CH_Y)))               # TL chamfer
    lines.append(((-1.0, 0.0), a))                                   # left
    n = (-CH_Y / nrm, -CH_X / nrm)
    lines.append((n, n[0] * (-a) + n[1] * (-b + CH_Y)))              # BL chamfer
    return [(n, c - d) for (n, c) in lines]


def poly_pts(d):
    lines = poly_lines(d)
    pts = []
    k = len(lines)
    for i in range(k):
        (n1, c1) = lines[i - 1]
        (n2, c2) = lines[i]
        det = n1[0] * n2[1] - n1[1] * n2[0]
        x = (c1 * n2[1] - c2 * n1[1]) / det
        y = (n1[0] * c2 - n2[0] * c1) / det
        pts.append((x, y))
    return pts  # pts[i] = start vertex of edge i (CCW)


def rounded_wire(d, r, z=0.0):
    """closed wire of the outline offset inward by d with corner radius r,
    starting at the middle of the bottom (-Y) edge, running CCW"""
    pts = poly_pts(d)
    k = len(pts)
    V = lambda p: cq.Vector(p[0], p[1], z)
    corners = []
    for i in range(k):
        p = pts[i]
        pin = pts[i - 1]
        pout = pts[(i + 1) % k]
        u1 = (p[0] - pin[0], p[1] - pin[1])
        l1 = math.hypot(*u1)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (pout[0] - p[0], pout[1] - p[1])
        l2 = math.hypot(*u2)
        u2 = (u2[0] / l2, u2[1] / l2)
        cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        th = math.acos(cosang)
        if r <= 1e-6 or th < 1e-6:
            corners.append((p, None, None))
            continue
        t = r * math.tan(th / 2.0)
        ta = (p[0] - u1[0] * t, p[1] - u1[1] * t)
        tb = (p[0] + u2[0] * t, p[1] + u2[1] * t)
        bis = (-u1[0] + u2[0], -u1[1] + u2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        dc = r / math.cos(th / 2.0)
        mid = (p[0] + bis[0] * (dc - r), p[1] + bis[1] * (dc - r))
        corners.append((ta, mid, tb))
    p0, p1 = pts[0], pts[1]
    start = ((p0[0] + p1[0]) / 2.0, (p0[1] + p1[1]) / 2.0)
    edges = []
    cur = start
    for i in list(range(1, k)) + [0]:
        ta, mid, tb = corners[i]
        edges.append(cq.Edge.makeLine(V(cur), V(ta)))
        if mid is None:
            cur = ta
        else:
            edges.append(cq.Edge.makeThreePointArc(V(ta), V(mid), V(tb)))
            cur = tb
    edges.append(cq.Edge.makeLine(V(cur), V(start)))
    return cq.Wire.assembleEdges(edges), start


def prism(d, r, z0, z1):
    w, _ = rounded_wire(d, r, z0)
    f = cq.Face.makeFromWires(w)
    return cq.Solid.extrudeLinear(f, cq.Vector(0, 0, z1 - z0))


def box_sel(x0, y0, z0, x1, y1, z1):
    return cq.selectors.BoxSelector((x0, y0, z0), (x1, y1, z1))


# ---------------- outer body ----------------
outer = cq.Workplane("XY").add(prism(0.0, 0.0, 0.0, Z_WALL))

# bottom rounding: sweep a cutter profile (arc tangent to the wall, meeting
# the underside at an angle) around the whole outline (mitred at corners)
path, st = rounded_wire(0.0, 0.0, 0.0)
y0 = st[1]  # = -W/2
Rarc = (BOT_ARC_Z ** 2 + BOT_ARC_IN ** 2) / (2.0 * BOT_ARC_IN)
angB = math.atan2(-BOT_ARC_Z, BOT_ARC_IN - Rarc)     # end angle (3rd quadrant)
angM = (math.pi + (angB + 2 * math.pi)) / 2.0
mid = (y0 + Rarc + Rarc * math.cos(angM), BOT_ARC_Z + Rarc * math.sin(angM))
P = lambda yy, zz: cq.Vector(st[0], yy, zz)
prof = cq.Wire.assembleEdges([
    cq.Edge.makeThreePointArc(P(y0, BOT_ARC_Z), P(*mid), P(y0 + BOT_ARC_IN, 0.0)),
    cq.Edge.makeLine(P(y0 + BOT_ARC_IN, 0.0), P(y0 + BOT_ARC_IN, -1.0)),
    cq.Edge.makeLine(P(y0 + BOT_ARC_IN, -1.0), P(y0 - 1.0, -1.0)),
    cq.Edge.makeLine(P(y0 - 1.0, -1.0), P(y0 - 1.0, BOT_ARC_Z)),
    cq.Edge.makeLine(P(y0 - 1.0, BOT_ARC_Z), P(y0, BOT_ARC_Z)),
])
ring = cq.Solid.sweep(prof, [], path, makeSolid=True, isFrenet=False,
                      transitionMode="right")
body = outer.cut(cq.Workplane("XY").add(ring))
# soften the vertical corners (fillet runs down the mitred bottom corners)
body = body.edges("|Z").fillet(R_CORNER)
body = body.faces(">Z").edges().fillet(TOP_EDGE_R)

# top lip (stepped in from the outer wall)
lip = prism(LEDGE, LIP_CORNER_R, Z_WALL - 0.5, H)
body = body.union(cq.Workplane("XY").add(lip))

# main cavity
cav = cq.Workplane("XY").add(prism(WALL, 0.0, FLOOR_T, H + 2.0))
cav = cav.edges("|Z").fillet(CAV_CORNER_R)
cav = cav.faces("<Z").edges().fillet(FLOOR_FILLET)
body = body.cut(cav)


# ---------------- bosses ----------------
def boss_solid(x, y):
    rb = BOSS_D / 2.0
    f = BOSS_BASE_R
    z0 = FLOOR_T - 0.6
    prof = (cq.Workplane("XZ")
            .moveTo(0, z0)
            .lineTo(rb + f, z0)
            .lineTo(rb + f, FLOOR_T)
            .radiusArc((rb, FLOOR_T + f), f)
            .lineTo(rb, BOSS_TOP - BOSS_TOP_R)
            .radiusArc((rb - BOSS_TOP_R, BOSS_TOP), -BOSS_TOP_R)
            .lineTo(PIN_D / 2.0, BOSS_TOP)
            .lineTo(PIN_D / 2.0, PIN_TOP)
            .lineTo(0, PIN_TOP)
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))
    return prof.val().translate(cq.Vector(x, y, 0))


boss_pts = [(bx, by) for bx in (BOSS_X_L, BOSS_X_R) for by in (BOSS_Y_POS, BOSS_Y_NEG)]
for (bx, by) in boss_pts:
    body = body.union(cq.Workplane("XY").add(boss_solid(bx, by)))

holes = (cq.Workplane("XY").workplane(offset=PIN_HOLE_BOT)
         .pushPoints(boss_pts).circle(PIN_HOLE_D / 2.0).extrude(PIN_TOP))
body = body.cut(holes)

# ---------------- floor features ----------------
# rectangular window (top edge rounded, bottom edge chamfered)
win = (cq.Workplane("XY").workplane(offset=-1.0).center(WIN_CX, WIN_CY)
       .rect(WIN_W, WIN_H).extrude(FLOOR_T + 2.0).edges("|Z").fillet(WIN_R))
body = body.cut(win)
wx0, wx1 = WIN_CX - WIN_W / 2 - 1, WIN_CX + WIN_W / 2 + 1
wy0, wy1 = WIN_CY - WIN_H / 2 - 1, WIN_CY + WIN_H / 2 + 1
body = body.edges(box_sel(wx0, wy0, FLOOR_T - 0.05, wx1, wy1, FLOOR_T + 0.05)).fillet(WIN_EDGE_R)
body = body.edges(box_sel(wx0, wy0, -0.05, wx1, wy1, 0.05)).chamfer(WIN_BOT_CH)

# square recess + round hole (chamfered underneath)
sq = (cq.Workplane("XY").workplane(offset=FLOOR_T - SQ_DEPTH).center(SQ_CX, SQ_CY)
      .rect(SQ_W, SQ_H).extrude(SQ_DEPTH + 1.0).edges("|Z").fillet(SQ_R))
body = body.cut(sq)
hole = (cq.Workplane("XY").workplane(offset=-1.0).center(SQ_CX, SQ_CY)
        .circle(HOLE_D / 2.0).extrude(FLOOR_T + 2.0))
body = body.cut(hole)
hr = HOLE_D / 2 + 0.5
body = body.edges(box_sel(SQ_CX - hr, SQ_CY - hr, -0.05,
                          SQ_CX + hr, SQ_CY + hr, 0.05)).chamfer(HOLE_BOT_CH)

# hex pocket (nut trap) + channel towards the back wall
hexp = (cq.Workplane("XY").workplane(offset=FLOOR_T - HEX_DEPTH)
        .center(HEX_CX, HEX_CY).transformed(rotate=(0, 0, 90))
        .polygon(6, 2 * HEX_R).extrude(HEX_DEPTH + 1.0))
body = body.cut(hexp)
chan = (cq.Workplane("XY").workplane(offset=FLOOR_T - CHAN_DEPTH)
        .center((CHAN_X0 + CHAN_X1) / 2.0, (HEX_CY + CHAN_Y1) / 2.0)
        .rect(CHAN_X1 - CHAN_X0, CHAN_Y1 - HEX_CY).extrude(CHAN_DEPTH + 1.0))
body = body.cut(chan)

# vent slots (through)
for (p, q) in SLOTS:
    cxs, cys = (p[0] + q[0]) / 2.0, (p[1] + q[1]) / 2.0
    ln = math.hypot(q[0] - p[0], q[1] - p[1])
    ang = math.degrees(math.atan2(q[1] - p[1], q[0] - p[0]))
    sl = (cq.Workplane("XY").workplane(offset=-1.0).center(cxs, cys)
          .transformed(rotate=(0, 0, ang)).slot2D(ln + SLOT_W, SLOT_W)
          .extrude(FLOOR_T + 2.0))
    body = body.cut(sl)

# ---------------- underside logo recesses ----------------
# +X end: hexagon + channel recess with a raised diagonal cross left standing
lx, ly, lr = LOGO1
logo1 = (cq.Workplane("XY").workplane(offset=-1.0).center(lx, ly)
         .transformed(rotate=(0, 0, 90)).polygon(6, 2 * lr)
         .extrude(1.0 + LOGO_DEPTH))
logo1c = (cq.Workplane("XY").workplane(offset=-1.0)
          .center((CHAN_X0 + CHAN_X1) / 2.0, (ly + CHAN_Y1) / 2.0)
          .rect(CHAN_X1 - CHAN_X0, CHAN_Y1 - ly).extrude(1.0 + LOGO_DEPTH))
cross = None
for a in (45.0, 135.0):
    arm = (cq.Workplane("XY").workplane(offset=-2.0).center(lx, ly)
           .transformed(rotate=(0, 0, a)).rect(CROSS_L, CROSS_W).extrude(4.0))
    cross = arm if cross is None else cross.union(arm)
body = body.cut(logo1.union(logo1c).cut(cross))

# -X end: hexagon recess with raised "dld" letter strokes left standing.
# text baseline runs parallel to a pair of hexagon edges (30 deg)
lx, ly, lr = LOGO2
logo2 = (cq.Workplane("XY").workplane(offset=-1.0).center(lx, ly)
         .transformed(rotate=(0, 0, 90)).polygon(6, 2 * lr)
         .extrude(1.0 + LOGO_DEPTH))
ua = math.radians(LOGO_TEXT_ANG)
uvec = (math.cos(ua), math.sin(ua))
vvec = (math.cos(ua - math.pi / 2), math.sin(ua - math.pi / 2))


def text_rect(u0, u1, v0, v1):
    cu, cv = (u0 + u1) / 2.0, (v0 + v1) / 2.0
    cx = lx + uvec[0] * cu + vvec[0] * cv
    cy = ly + uvec[1] * cu + vvec[1] * cv
    return (cq.Workplane("XY").workplane(offset=-2.0).center(cx, cy)
            .transformed(rotate=(0, 0, LOGO_TEXT_ANG))
            .rect(u1 - u0, v1 - v0).extrude(4.0))


half_h = lr * math.sqrt(3.0) / 2.0
strokes = [
    text_rect(-0.5, 0.5, -half_h - 0.5, half_h + 0.5),        # l
]
for (b0, st0) in ((-5.0, -3.1), (2.2, 4.1)):                 # two d's
    st1 = st0 + STROKE
    strokes.append(text_rect(st0, st1, -4.0, 4.0))            # stem
    strokes.append(text_rect(b0, st0, 0.4, 0.4 + STROKE))     # bowl top
    strokes.append(text_rect(b0, st0, -4.0, -4.0 + STROKE))   # bowl bottom
    strokes.append(text_rect(b0, b0 + STROKE, -4.0, 0.4 + STROKE))  # bowl side
letters = strokes[0]
for s_ in strokes[1:]:
    letters = letters.union(s_)
body = body.cut(logo2.cut(letters))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
